import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 80.0            # overall width (Y)
H = 120.0           # overall height (Z)
T = 11.5            # plate thickness (X)
TAB_W = 40.0        # width of the lower tab (at -Y side)
STEP_Z = 35.4       # height of the tab / underside of the main body
CH = 2.4            # corner chamfer of the outline

GROOVE_R = 14.5     # pipe groove radius
GROOVE_DEPTH = 6.4  # depth of groove into +X face
GROOVE_Z = [H - 23.0, H - 63.0]   # groove axis heights

SLOT_L = 7.0        # slot length (Y)
SLOT_H = 3.4        # slot height (Z)
SLOT_OFF = 16.5     # slot offset above/below groove axis
SLOT_Y = [-W / 2 + 9.2, W / 2 - 7.0]

TEXT = "FDM-0000-00"   # engraved part number (reads upside-down on +X face)
TEXT_SIZE = 6.7
TEXT_DEPTH = 0.5
TEXT_Y = 1.0
TEXT_Z = 77.8

HOLE_D = 6.5
HOLE_Z = 17.0
HOLE_Y = [-W / 2 + 11.5, -W / 2 + 28.5]

# ---------------- base L-shaped plate ----------------
y0, y1, yt = -W / 2, W / 2, -W / 2 + TAB_W
pts = [
    (y0 + CH, 0.0),
    (yt - CH, 0.0),
    (yt, CH),
    (yt, STEP_Z),
    (y1 - CH, STEP_Z),
    (y1, STEP_Z + CH),
    (y1, H - CH),
    (y1 - CH, H),
    (y0 + CH, H),
    (y0, H - CH),
    (y0, CH),
]
plate = (
    cq.Workplane("YZ", origin=(-T / 2, 0, 0))
    .polyline(pts)
    .close()
    .extrude(T)
)

# ---------------- pipe grooves on the +X face ----------------
for gz in GROOVE_Z:
    cyl = (
        cq.Workplane("XZ", origin=(0, W / 2 + 1, 0))
        .center(T / 2 + GROOVE_R - GROOVE_DEPTH, gz)
        .circle(GROOVE_R)
        .extrude(W + 2)
    )
    plate = plate.cut(cyl)

# ---------------- cable-tie slots (through) ----------------
slot_pts = []
for gz in GROOVE_Z:
    for dz in (SLOT_OFF, -SLOT_OFF):
        for sy in SLOT_Y:
            slot_pts.append((sy, gz + dz))
slots = (
    cq.Workplane("YZ", origin=(-T / 2 - 1, 0, 0))
    .pushPoints(slot_pts)
    .rect(SLOT_L, SLOT_H)
    .extrude(T + 2)
)
plate = plate.cut(slots)

# ---------------- mounting holes in the tab ----------------
# (workplane x-dir = +Z keeps the cylinder seam on the hidden upper wall)
hole_plane = cq.Plane(origin=(-T / 2 - 1, 0, 0), xDir=(0, 0, 1), normal=(1, 0, 0))
holes = (
    cq.Workplane(hole_plane)
    .pushPoints([(HOLE_Z, -hy) for hy in HOLE_Y])   # local y = -Y
    .circle(HOLE_D / 2)
    .extrude(T + 2)
)
plate = plate.cut(holes)

# ---------------- engraved part number on the middle land ----------------
txt_plane = cq.Plane(origin=(T / 2, TEXT_Y, TEXT_Z), xDir=(0, -1, 0), normal=(1, 0, 0))
try:
    engraving = cq.Workplane(txt_plane).text(
        TEXT, TEXT_SIZE, -TEXT_DEPTH, combine=False, halign="center", valign="center"
    )
    engraved = plate.cut(engraving)
    if engraved.val().isValid() and len(engraved.solids().vals()) == 1:
        plate = engraved
except Exception:
    pass  # keep the plain plate if no font is available

result = plate
